import math
import cadquery as cq
from OCP.TopTools import TopTools_IndexedDataMapOfShapeListOfShape
from OCP.TopExp import TopExp
from OCP.TopAbs import TopAbs_EDGE, TopAbs_FACE
from OCP.BRepAdaptor import BRepAdaptor_Surface

# ---------------- driving dimensions (mm) ----------------
H = 119.25          # overall height (Z)
T_PLATE = 11.25     # plate thickness at the spline end (X)
D_THICK = 22.0      # thickness of the upper handle part (X)

# back rounding: radius about the Z axis through the front-face centre line
R_TOP = 19.9                      # at the top face
Z_UB, R_UB = 97.2, 23.75          # upper bulge (at the upper hole)
Z_WAIST, R_WAIST = 70.75, 23.0    # at the waist
Z_LB, R_LB = 45.25, 24.0          # lower bulge of the front outline
Z_RCYL = 40.0                     # back rounding is cylindrical (R_LB) below this
Z_R2, R_R2 = 52.0, 23.3           # back rounding just above the lower bulge
Z_C = R_LB                        # centre of the bottom round end / spline

# front outline (Y half widths)
W_WAIST = 20.2
BLEND_R = 4.0                     # blend between flat side walls and rounded back

# pocket on the back around the spline (leaves the thin plate)
Z_POCKET_C = 22.7
R_POCKET = 28.3
FLOOR_FILLET = 2.6
SIDE_FILLET = 1.5
POCKET_EDGE_R = 1.0           # rounding of the top edge of the pocket wall

# top bore with keyway (bore centred on the front face)
BORE_R_TOP = 11.5             # slightly tapered bore
BORE_R_BOT = 10.9
BORE_DEPTH = 11.6
BORE_FILLET = 1.2             # at the bottom of the bore
BORE_CHAMFER = 0.7            # at the top of the bore / keyway
KEY_W = 4.3
KEY_X = 14.2                  # keyway bottom distance from the front face
TOP_CHAMFER = 0.7

# small holes
HOLE_Z = (97.0, 58.5)
HOLE_D = 4.0
CSK_D = 6.5
CB_D = 13.5
CB_DEPTH = 2.5

# internal spline
SPL_N = 15
SPL_R_MIN = 9.5
SPL_R_MAJ = 12.6
SPL_GROOVE_W = 2.3
SPL_TIP_R = 0.7               # rounding of the tooth tips

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- helpers ----------------
def edge_face_map(shape):
    m = TopTools_IndexedDataMapOfShapeListOfShape()
    TopExp.MapShapesAndAncestors_s(shape.wrapped, TopAbs_EDGE, TopAbs_FACE, m)
    res = []
    for i in range(1, m.Extent() + 1):
        res.append((cq.Edge(m.FindKey(i)), [cq.Face(f) for f in m.FindFromIndex(i)]))
    return res


def is_side_wall(face):
    """face generated by extruding the outline along X (normal has no X part)"""
    if face.geomType() == "PLANE":
        n = face.normalAt()
        return abs(n.x) < 1e-6 and abs(n.z) < 0.99
    u0, u1, v0, v1 = face._uvBounds()
    for a in (0.2, 0.5, 0.8):
        for b in (0.2, 0.5, 0.8):
            n, _ = face.normalAt(u0 + a * (u1 - u0), v0 + b * (v1 - v0))
            if abs(n.x) > 1e-6:
                return False
    return True


# ---------------- rounded back (revolved) ----------------
rev = (
    cq.Workplane("XZ")
    .moveTo(0, -1)
    .lineTo(R_LB, -1)
    .lineTo(R_LB, Z_RCYL)
    .spline([(R_R2, Z_R2), (R_WAIST, Z_WAIST), (R_UB, Z_UB)],
            tangents=[(0.0, 1.0), (0.05, 1.0)], includeCurrent=True)
    .lineTo(R_TOP, H)
    .lineTo(0, H)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)

# ---------------- front outline extruded through the thickness ----------------
ext = (
    cq.Workplane("YZ").workplane(offset=-D_THICK)
    .moveTo(0, H + 1)
    .lineTo(R_TOP + 0.6, H + 1)
    .lineTo(R_UB + 0.3, Z_UB + 0.5)
    .lineTo(W_WAIST + 0.4, 80.0)
    .spline(
        [(W_WAIST, Z_WAIST), (W_WAIST + 0.8, 60.0), (R_LB - 1.0, 51.75), (R_LB + 0.5, Z_LB - 3)],
        tangents=[(-0.2, -1.0), (0.0, -1.0)],
        includeCurrent=True,
    )
    .lineTo(R_LB + 0.5, Z_C)
    .lineTo(R_LB, Z_C)
    .threePointArc((R_LB * math.sin(math.pi / 4), Z_C - R_LB * math.cos(math.pi / 4)), (0, 0))
    .mirrorY()
    .extrude(D_THICK)
)

body = rev.intersect(ext).val()

# blend the creases between the flat side walls and the rounded back
creases = []
for e, fs in edge_face_map(body):
    if len(fs) != 2:
        continue
    w = [is_side_wall(f) for f in fs]
    if w[0] != w[1]:
        other = fs[1] if w[0] else fs[0]
        if other.geomType() != "PLANE" and e.Center().z > Z_RCYL:
            creases.append(e)
if creases:
    try:
        body = body.fillet(BLEND_R, creases)
    except Exception:
        pass

# pocket behind the spline (its foot rounded by a filleted cutter)
pocket = (
    cq.Workplane("YZ").workplane(offset=-D_THICK - 1)
    .center(0, Z_POCKET_C).circle(R_POCKET).extrude(D_THICK + 1 - T_PLATE)
)
try:
    pocket = pocket.faces(">X").edges().fillet(FLOOR_FILLET)
except Exception:
    pass
body = body.cut(pocket.val())


def floor_edges(shape, kind):
    out = []
    for e, fs in edge_face_map(shape):
        if e.geomType() != kind or any(f.geomType() == "TORUS" for f in fs):
            continue
        if any(f.geomType() == "PLANE" and abs(f.normalAt().x + 1) < 1e-6
               and abs(f.Center().x + T_PLATE) < 1e-3 for f in fs):
            out.append(e)
    return out


# round the outer edges of the pocket floor (bottom end, then the sides)
for kind, rad in (("CIRCLE", FLOOR_FILLET), ("LINE", SIDE_FILLET)):
    es = floor_edges(body, kind)
    if es:
        try:
            body = body.fillet(rad, es)
        except Exception:
            pass

# round the upper (outer) edge of the pocket wall
_wall = None
for f in body.Faces():
    if f.geomType() == "CYLINDER":
        cyl = BRepAdaptor_Surface(f.wrapped).Cylinder()
        if abs(cyl.Radius() - R_POCKET) < 1e-3 and abs(abs(cyl.Axis().Direction().X()) - 1) < 1e-6:
            _wall = f
if _wall is not None:
    _wall_edges = [e for e, fs in edge_face_map(body)
                   if any(f.isSame(_wall) for f in fs) and not any(f.geomType() == "TORUS" for f in fs)]
    try:
        body = body.fillet(POCKET_EDGE_R, _wall_edges)
    except Exception:
        pass

body = cq.Workplane().add(body)

# chamfer on the outer (rounded) top edge
try:
    body = body.faces(">Z").edges("not %LINE").chamfer(TOP_CHAMFER)
except Exception:
    pass

# ---------------- top bore + keyway ----------------
bore = cq.Workplane().add(
    cq.Solid.makeCone(BORE_R_BOT, BORE_R_TOP + (BORE_R_TOP - BORE_R_BOT) / BORE_DEPTH,
                      BORE_DEPTH + 1, pnt=cq.Vector(0, 0, H - BORE_DEPTH))
)
key = (
    cq.Workplane("XY").workplane(offset=H - BORE_DEPTH)
    .center(-KEY_X / 2, 0)
    .rect(KEY_X, KEY_W).extrude(BORE_DEPTH + 1)
)
cutter = bore.union(key)
try:
    cutter = cutter.faces("<Z").edges().fillet(BORE_FILLET)
except Exception:
    pass
body = body.cut(cutter)

# chamfer the top edges of the bore and keyway
def _bore_top_edge(e):
    p = e.positionAt(0.5)
    if abs(p.z - H) > 1e-3 or abs(e.startPoint().z - H) > 1e-3:
        return False
    in_bore = math.hypot(p.x, p.y) <= BORE_R_TOP + 0.05 and p.x < -0.05
    in_key = p.x <= -BORE_R_TOP + 1.0 and abs(p.y) <= KEY_W / 2 + 0.05
    return in_bore or in_key


_top_edges = [e for e in body.edges().vals() if _bore_top_edge(e)]
if _top_edges:
    try:
        body = cq.Workplane().add(body.val().chamfer(BORE_CHAMFER, None, _top_edges))
    except Exception:
        pass

# ---------------- small holes ----------------
for hz in HOLE_Z:
    h = (cq.Workplane("YZ").workplane(offset=-D_THICK - 1).center(0, hz)
         .circle(HOLE_D / 2).extrude(D_THICK + 2))
    cb = (cq.Workplane("YZ").workplane(offset=-D_THICK - 1).center(0, hz)
          .circle(CB_D / 2).extrude(CB_DEPTH + 1))
    csk = cq.Solid.makeCone(CSK_D / 2 + 0.01, HOLE_D / 2 - 0.01, (CSK_D - HOLE_D) / 2 + 0.02,
                            pnt=cq.Vector(0.01, 0, hz), dir=cq.Vector(-1, 0, 0))
    body = body.cut(h).cut(cb).cut(cq.Workplane().add(csk))

# ---------------- internal spline ----------------
spl = (cq.Workplane("YZ").workplane(offset=-T_PLATE - 1).center(0, Z_C)
       .circle(SPL_R_MIN).extrude(T_PLATE + 2))
for i in range(SPL_N):
    a = 2 * math.pi * i / SPL_N          # angle from +Y axis toward +Z
    L = SPL_R_MAJ - SPL_GROOVE_W / 2 - (SPL_R_MIN - 1.0)
    rmid = (SPL_R_MIN - 1.0) + L / 2
    slot = (cq.Workplane("YZ").workplane(offset=-T_PLATE - 1)
            .center(rmid * math.cos(a), Z_C + rmid * math.sin(a))
            .slot2D(L + SPL_GROOVE_W, SPL_GROOVE_W, math.degrees(a))
            .extrude(T_PLATE + 2))
    spl = spl.union(slot)
body = body.cut(spl)


def _tooth_tip(e):
    if e.geomType() != "LINE":
        return False
    a, b = e.startPoint(), e.endPoint()
    if abs(a.y - b.y) > 1e-6 or abs(a.z - b.z) > 1e-6:
        return False
    return abs(math.hypot(a.y, a.z - Z_C) - SPL_R_MIN) < 0.05


_tips = [e for e in body.edges().vals() if _tooth_tip(e)]
if _tips:
    try:
        body = cq.Workplane().add(body.val().fillet(SPL_TIP_R, _tips))
    except Exception:
        pass

result = body
